import math
import cadquery as cq

# =====================================================================
# Honeycomb bracket / tray: base plate with hexagonal lightening cells,
# a tall back wall and a front wall joined to the base by large fillets,
# a central pocket with a rectangular window, two pairs of pins, a square
# cup and counterbored mounting holes through the back wall.
# X = length, Y = width (front = -Y, back = +Y), Z = height.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 50.0          # overall width (Y)
H = 20.6          # overall height (Z)
TB = 4.2          # base plate thickness
T = 4.0           # wall thickness
RF = 6.0          # fillet radius wall/base (inside)

P = 22.2          # honeycomb pitch (X)
F = 17.9          # hex cell flat-to-flat
RS = P * math.sqrt(3) / 2.0   # row spacing (Y)
RIM = 3.6         # rim around the end cells

X_TIP = 5.5 * P + F / 2 + RIM                    # end tip of the base plate
TIP_HALF = 7.9    # half-length of the vertical flat at the tips
X_BW = 124.0      # back wall half length
X_FW_END = X_TIP - (W / 2 - TIP_HALF) / math.tan(math.radians(30)) + T / math.tan(math.radians(30))
                  # front wall end (where the inner face meets the end diagonal)
R_FW_END = 5.0    # rounding of the top corners of the front wall ends
R_TOPC = 3.0      # rounding of top corners of back wall ends

BAND = 27.0       # central solid band half-length (cells clipped here)
Y_IN = W / 2 - T  # inner face of walls

# central pocket / window
PL_X = 21.0             # raised platform half length
PL_Y0 = -18.5           # platform front edge (meets the front fillet)
PL_Z = 5.3              # platform top
RC_X = 20.7             # recess of the back wall inner face
RC_D = 0.9
PK_X = 18.8             # inner pocket half length
PK_Y0, PK_Y1 = -15.8, Y_IN + RC_D
PK_Z = 2.7              # pocket floor
WIN_RIM = 0.6           # stepped rim around the window
WIN_STEP = 0.6
WIN_BOT = 3.5           # chamfered recess around the window on the underside
WIN_BOT_D = 1.4
WIN_X = 14.8
WIN_Y0, WIN_Y1 = -3.8, 13.4
PAD_X = 15.7
PAD_Y = (18.9, -13.1)
PAD_R = 3.4
PAD_HOLE = 2.0

# pins
BOSS_X = 32.0
BOSS_Y = (7.2, -8.2)
BOSS_D = 6.4
BOSS_H = 10.5
BOSS_HOLE = 2.0

# square cup
CUP_X = -50.0
CUP_Y = 0.0
CUP_A = 20.5
CUP_B = 20.0
CUP_H = 11.4
CUP_WALL = 1.6
CUP_FLOOR = 7.5
CUP_HOLE_D = 10.5
CUP_BOT_D = 11.0        # shallow round recess under the cup
CUP_BOT_DEPTH = 0.7

# back-wall mounting holes
HOLE_Z = 10.4
HOLE_XS = (-111.2, -22.0, 22.0, 111.2)
HOLE_D = 3.2
CB_D = 6.0
CB_DEPTH = 2.0
SF_D = 9.2
SF_DEPTH = 0.4

# small blind slots on the inner face of the back wall
SLOT_L = 5.8
SLOT_H = 1.5
SLOT_DEPTH = 0.8
SLOT_Z = (17.3, 10.6)

TAN30 = math.tan(math.radians(30))

# ---------------- base plate outline ----------------
y_diag_bw = TIP_HALF + (X_TIP - X_BW) * TAN30
x_front = X_TIP - (W / 2 - TIP_HALF) / TAN30
outline = [
    (-X_BW, W / 2), (X_BW, W / 2), (X_BW, y_diag_bw), (X_TIP, TIP_HALF),
    (X_TIP, -TIP_HALF), (x_front, -W / 2), (-x_front, -W / 2),
    (-X_TIP, -TIP_HALF), (-X_TIP, TIP_HALF), (-X_BW, y_diag_bw),
]
base = cq.Workplane("XY").polyline(outline).close().extrude(TB)
outline_prism = cq.Workplane("XY").polyline(outline).close().extrude(H)


# ---------------- walls with inner fillets (YZ profile extruded along X) ----------------
def wall_profile(sign):
    """Wall + fillet profile in the YZ plane; sign=+1 back wall, -1 front wall."""
    yo = sign * W / 2
    yi = sign * Y_IN
    yf = sign * (Y_IN - RF)
    c45 = math.cos(math.radians(45))
    ym = sign * (Y_IN - RF + RF * c45)
    zm = TB + RF - RF * c45
    return (cq.Workplane("YZ")
            .moveTo(yo, 0).lineTo(yo, H).lineTo(yi, H).lineTo(yi, TB + RF)
            .threePointArc((ym, zm), (yf, TB))
            .lineTo(yf, 0).close())


def back_wall():
    s = wall_profile(+1).extrude(X_BW, both=True)
    s = s.edges("|Y").edges(">Z").fillet(R_TOPC)
    return s


def front_wall():
    s = wall_profile(-1).extrude(X_TIP, both=True)
    # end of the wall above the fillet: rounded top corner in elevation
    upper = (cq.Workplane("XZ").rect(2 * X_FW_END, H).extrude(-W - 2)
             .translate((0, -W / 2 - 1, H / 2))
             .edges("|Y").edges(">Z").fillet(R_FW_END))
    lower = cq.Workplane("XY").box(2 * X_TIP + 2, W + 2, TB + RF).translate((0, 0, (TB + RF) / 2))
    return s.intersect(upper.union(lower))


body = base.union(back_wall()).union(front_wall())
body = body.intersect(outline_prism)


# ---------------- honeycomb cut ----------------
CELL_R = 1.2      # rounding of the vertical cell corners


def clip_poly(poly, a, b, c):
    """Sutherland-Hodgman: keep the part of poly where a*x + b*y <= c."""
    out = []
    n = len(poly)
    for i in range(n):
        p, q = poly[i], poly[(i + 1) % n]
        fp = a * p[0] + b * p[1] - c
        fq = a * q[0] + b * q[1] - c
        if fp <= 0:
            out.append(p)
        if fp * fq < 0:
            t = fp / (fp - fq)
            out.append((p[0] + t * (q[0] - p[0]), p[1] + t * (q[1] - p[1])))
    return out


def cell_cutter(xc, yc):
    r = F / math.sqrt(3)
    poly = [(xc + r * math.cos(math.radians(90 + 60 * i)), yc + r * math.sin(math.radians(90 + 60 * i)))
            for i in range(6)]
    sx = 1 if xc > 0 else -1
    n30, s30 = math.cos(math.radians(30)), math.sin(math.radians(30))
    half_planes = [
        (0, 1, Y_IN), (0, -1, Y_IN),                     # walls
        (-sx, 0, -BAND),                                  # central band
        (sx, 0, X_TIP - RIM),                             # tip flat
        (sx * s30, -n30, TIP_HALF * n30 + X_TIP * s30 - RIM),   # lower diagonal
    ]
    if yc > 0:
        half_planes.append((sx, 0, X_BW - RIM))          # end of the back wall
    else:
        half_planes.append((sx * s30, n30, TIP_HALF * n30 + X_TIP * s30 - RIM))  # upper diagonal
    for (a, b, c) in half_planes:
        poly = clip_poly(poly, a, b, c)
        if len(poly) < 3:
            return None
    # drop near-duplicate points
    clean = []
    for p in poly:
        if not clean or math.hypot(p[0] - clean[-1][0], p[1] - clean[-1][1]) > 1e-3:
            clean.append(p)
    if math.hypot(clean[0][0] - clean[-1][0], clean[0][1] - clean[-1][1]) < 1e-3:
        clean.pop()
    area = 0.5 * abs(sum(clean[i][0] * clean[(i + 1) % len(clean)][1] - clean[(i + 1) % len(clean)][0] * clean[i][1]
                         for i in range(len(clean))))
    if area < 1.0:
        return None
    for rr in (CELL_R, 0.6, 0.0):
        try:
            sk = cq.Sketch().polygon(clean + [clean[0]])
            if rr > 0:
                sk = sk.vertices().fillet(rr)
            w = cq.Workplane("XY").placeSketch(sk).extrude(H + 20).translate((0, 0, -10))
            if w.val().isValid():
                return w
        except Exception:
            pass
    return None


centers = []
for k in range(1, 6):
    for sx in (-1, 1):
        centers.append((sx * k * P, RS))
        centers.append((sx * k * P, -RS))
        centers.append((sx * (k + 0.5) * P, 0.0))
cells = None
for (xc, yc) in centers:
    cc = cell_cutter(xc, yc)
    if cc is None:
        continue
    cells = cc if cells is None else cells.union(cc)
body = body.cut(cells)

# ---------------- central pocket with rectangular window ----------------
platform = cq.Workplane("XY").box(2 * PL_X, Y_IN - PL_Y0, PL_Z).translate((0, (Y_IN + PL_Y0) / 2, PL_Z / 2))
body = body.union(platform)
recess = cq.Workplane("XY").box(2 * RC_X, 2 * RC_D, H).translate((0, Y_IN, PK_Z + H / 2))
body = body.cut(recess)
pocket = cq.Workplane("XY").box(2 * PK_X, PK_Y1 - PK_Y0, H).translate((0, (PK_Y0 + PK_Y1) / 2, PK_Z + H / 2))
for px in (-PAD_X, PAD_X):
    for py in PAD_Y:
        edge_y = PK_Y1 if py > 0 else PK_Y0
        sxp = 1 if px > 0 else -1
        pad = cq.Workplane("XY").circle(PAD_R).extrude(PL_Z).translate((px, py, 0))
        blk = cq.Workplane("XY").box(2 * PAD_R, abs(edge_y - py) + 1, PL_Z).translate(
            (px, (py + edge_y) / 2, PL_Z / 2))
        blk2 = cq.Workplane("XY").box(PK_X - px * sxp + 1, 2 * PAD_R, PL_Z).translate(
            (sxp * (PK_X + abs(px)) / 2, py, PL_Z / 2))
        pocket = pocket.cut(pad.union(blk).union(blk2))
body = body.cut(pocket)
# window: through opening with a small step around it and a chamfered recess below
win_c = (0, (WIN_Y0 + WIN_Y1) / 2)
win_w, win_h = 2 * WIN_X, WIN_Y1 - WIN_Y0
window = cq.Workplane("XY").rect(win_w, win_h).extrude(40).translate((win_c[0], win_c[1], -10))
body = body.cut(window)
step = (cq.Workplane("XY").rect(win_w + 2 * WIN_RIM, win_h + 2 * WIN_RIM).extrude(WIN_STEP + 5)
        .edges("|Z").fillet(1.5).translate((win_c[0], win_c[1], PK_Z - WIN_STEP)))
body = body.cut(step)
bot = (cq.Workplane("XY").rect(win_w + 2 * WIN_BOT, win_h + 2 * WIN_BOT).extrude(WIN_BOT_D)
       .faces(">Z").edges().chamfer(WIN_BOT_D * 0.95).translate((win_c[0], win_c[1], 0)))
body = body.cut(bot.translate((0, 0, -0.001)))
for px in (-PAD_X, PAD_X):
    for py in PAD_Y:
        body = body.cut(cq.Workplane("XY").circle(PAD_HOLE / 2).extrude(40).translate((px, py, -10)))

# ---------------- cylindrical pins ----------------
for bx in (-BOSS_X, BOSS_X):
    for by in BOSS_Y:
        b = (cq.Workplane("XY").circle(BOSS_D / 2).extrude(BOSS_H).translate((bx, by, 0))
             .faces(">Z").edges().chamfer(0.6))
        body = body.union(b)
        body = body.cut(cq.Workplane("XY").circle(BOSS_HOLE / 2).extrude(5).translate((bx, by, BOSS_H - 4)))

# ---------------- square cup ----------------
cup = cq.Workplane("XY").box(CUP_A, CUP_B, CUP_H).translate((CUP_X, CUP_Y, CUP_H / 2))
cup = cup.cut(cq.Workplane("XY").box(CUP_A - 2 * CUP_WALL, CUP_B - 2 * CUP_WALL, CUP_H)
              .translate((CUP_X, CUP_Y, CUP_FLOOR + CUP_H / 2)))
body = body.union(cup)
body = body.cut(cq.Workplane("XY").circle(CUP_HOLE_D / 2).extrude(CUP_H).translate((CUP_X, CUP_Y + 0.5, 1.5)))
body = body.cut(cq.Workplane("XY").circle(CUP_BOT_D / 2).extrude(CUP_BOT_DEPTH + 1)
                .translate((CUP_X, CUP_Y + 0.5, -1)))
body = body.cut(cq.Workplane("XY").box(3.0, 3.0, CUP_H)
                .translate((CUP_X, CUP_Y + 0.5 + CUP_HOLE_D / 2, 1.5 + CUP_H / 2)))


# ---------------- back wall holes (spot face + counterbore from inside) ----------------
def y_cyl(d, y0, y1, x, z):
    """cylinder along Y from y0 to y1 (y1 > y0) at (x, z)"""
    return cq.Workplane("XZ").circle(d / 2).extrude(-(y1 - y0)).translate((x, y0, z))


for hx in HOLE_XS:
    body = body.cut(y_cyl(HOLE_D, Y_IN - 5, W / 2 + 1, hx, HOLE_Z))
    body = body.cut(y_cyl(CB_D, Y_IN - 1, Y_IN + CB_DEPTH, hx, HOLE_Z))
    body = body.cut(y_cyl(SF_D, Y_IN - 1, Y_IN + SF_DEPTH, hx, HOLE_Z))

# ---------------- small blind slots on the back wall inner face ----------------
for k in range(1, 5):
    for sx in (-1, 1):
        for sz in SLOT_Z:
            body = body.cut(cq.Workplane("XY").box(SLOT_L, 2 * SLOT_DEPTH, SLOT_H)
                            .translate((sx * (k + 0.5) * P, Y_IN, sz)))

# ---------------- thin grooves along the tops of the wall ribs ----------------
GROOVE_W = 0.6
GROOVE_D = 1.0


def rib_groove(sign, xr):
    yc = sign * (Y_IN - RF)
    zc = TB + RF
    c45 = math.cos(math.radians(45))
    r0, r1 = RF - 0.2, RF + GROOVE_D
    # ring sector (quarter) between r0 and r1 around the fillet centre, in the YZ plane
    prof = (cq.Workplane("YZ", origin=(xr - GROOVE_W / 2, 0, 0))
            .moveTo(yc + sign * r0, zc)
            .lineTo(yc + sign * r1, zc)
            .threePointArc((yc + sign * r1 * c45, zc - r1 * c45), (yc, zc - r1))
            .lineTo(yc, zc - r0)
            .threePointArc((yc + sign * r0 * c45, zc - r0 * c45), (yc + sign * r0, zc))
            .close())
    return prof.extrude(GROOVE_W)


for k in range(1, 5):
    for sx in (-1, 1):
        for sy in (-1, 1):
            body = body.cut(rib_groove(sy, sx * (k + 0.5) * P))

# ---------------- soften the exposed perimeter edges of the base plate ----------------
EDGE_R = 0.8


def _on_outline(p, tol=1e-3):
    n = len(outline)
    for i in range(n):
        (ax, ay), (bx, by) = outline[i], outline[(i + 1) % n]
        dx, dy = bx - ax, by - ay
        t = ((p.x - ax) * dx + (p.y - ay) * dy) / (dx * dx + dy * dy)
        if -1e-6 <= t <= 1 + 1e-6 and math.hypot(p.x - (ax + t * dx), p.y - (ay + t * dy)) < tol:
            return True
    return False


perim = []
for e in body.edges().vals():
    if e.geomType() != "LINE":
        continue
    p0, p1 = e.startPoint(), e.endPoint()
    if abs(p0.z - p1.z) > 1e-6 or not (abs(p0.z) < 1e-6 or abs(p0.z - TB) < 1e-6):
        continue
    if _on_outline(p0) and _on_outline(p1):
        perim.append(e)
try:
    rounded = body.newObject(perim).fillet(EDGE_R)
    if rounded.val().isValid():
        body = rounded
except Exception:
    pass

result = body
